import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R_BODY = 50.3          # main cylindrical housing radius
Z_BODY_BOT = 37.0      # bottom of main body (top of flange step)
Z_BODY_TOP = 165.1     # top face of main body
TOP_CHAMFER = 0.8

R_DISK = 39.3          # raised top disk (top radius)
H_DISK = 1.1
DISK_BEVEL = 0.9       # bevelled rim of the raised disk

# grooves on the housing (z_low, z_high, depth)
GROOVES = [
    (159.9, 161.1, 0.35),  # thin groove under the top cap
    (142.5, 145.8, 3.4),   # upper groove
    (57.0, 60.4, 3.4),     # lower groove
]

# bottom flange
R_STEP = 54.1          # upper flange step
Z_FLANGE_TOP = 33.75
R_FLANGE = 56.0
Z_FLANGE_BOT = 27.4

# lower spigot cylinder
R_LOWER = 44.3

# notch in flange underside at +X
NOTCH_HALF_W = 29.8
Z_NOTCH_TOP = 31.6

# key blocks on the spigot
BLK_Z0, BLK_Z1 = 12.8, 25.2
BLK_PX_OUT, BLK_PX_HW = 47.4, 20.4     # +X block: outer x, half width (Y)
BLK_NX_OUT, BLK_NX_HW = 50.2, 10.0     # -X block

# holes
R_TOP_CB = 46.5        # 4 counterbored holes on top rim
CB_R, CB_D, CB_HOLE_R, CB_HOLE_D = 3.3, 1.5, 1.7, 8.0
R_DISK_HOLES_AX = 27.7  # 4 holes on axes
R_DISK_HOLES_DG = 29.8  # 4 holes on diagonals
DISK_HOLE_R, DISK_HOLE_D = 2.4, 8.0
CENTER_TOP_R, CENTER_BOT_R, CENTER_D = 8.6, 6.8, 1.8   # tapered centre pocket

R_FL_HOLES = 51.0      # flange through holes at diagonals
FL_HOLE_R, FL_CB_R, FL_CB_D = 1.8, 4.7, 2.0
SEAM_ANGLE = 180.0     # put cylinder seams on the -X side


def cyl(r, z0, z1):
    return (cq.Workplane("XY").workplane(offset=z0).circle(r).extrude(z1 - z0)
            .rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE))


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


# ---------------- main body ----------------
body = cyl(R_BODY, Z_BODY_BOT, Z_BODY_TOP)
body = body.faces(">Z").edges().chamfer(TOP_CHAMFER)

for z0, z1, d in GROOVES:
    ring = cyl(R_BODY + 1, z0, z1).cut(cyl(R_BODY - d, z0, z1))
    body = body.cut(ring)

# raised disk on top
disk = cq.Solid.makeCone(R_DISK + DISK_BEVEL, R_DISK, H_DISK,
                         cq.Vector(0, 0, Z_BODY_TOP), cq.Vector(0, 0, 1))
disk = disk.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), SEAM_ANGLE)
body = body.union(cq.Workplane("XY").add(disk))

# ---------------- flange ----------------
flange = cyl(R_FLANGE, Z_FLANGE_BOT, Z_FLANGE_TOP).union(
    cyl(R_STEP, Z_FLANGE_TOP, Z_BODY_BOT))
notch = box(0, R_FLANGE + 5, -NOTCH_HALF_W, NOTCH_HALF_W,
            Z_FLANGE_BOT - 1, Z_NOTCH_TOP)
flange = flange.cut(notch)

# flange holes at diagonals, counterbored from below (cut before the body is
# added, so the part of each hole lying under the housing stays closed by it)
for a in (45, 135, 225, 315):
    x, y = R_FL_HOLES * math.cos(math.radians(a)), R_FL_HOLES * math.sin(math.radians(a))
    flange = flange.cut(cyl(FL_HOLE_R, Z_FLANGE_BOT - 1, Z_BODY_BOT + 1).translate((x, y, 0)))
    flange = flange.cut(cyl(FL_CB_R, Z_FLANGE_BOT - 1, Z_FLANGE_BOT + FL_CB_D).translate((x, y, 0)))

# ---------------- lower spigot + blocks ----------------
lower = cyl(R_LOWER, 0, Z_BODY_BOT)
blk_p = box(R_LOWER - 6, BLK_PX_OUT, -BLK_PX_HW, BLK_PX_HW, BLK_Z0, BLK_Z1)
blk_n = box(-BLK_NX_OUT, -(R_LOWER - 6), -BLK_NX_HW, BLK_NX_HW, BLK_Z0, BLK_Z1)

part = body.union(flange).union(lower).union(blk_p).union(blk_n)

# ---------------- holes ----------------
ztop = Z_BODY_TOP
# counterbored holes on top rim (on axes)
pts = [(R_TOP_CB * math.cos(math.radians(a)), R_TOP_CB * math.sin(math.radians(a)))
       for a in (0, 90, 180, 270)]
for x, y in pts:
    part = part.cut(cyl(CB_R, ztop - CB_D, ztop + 5).translate((x, y, 0)))
    part = part.cut(cyl(CB_HOLE_R, ztop - CB_HOLE_D, ztop).translate((x, y, 0)))

# 8 holes on raised disk
zd = Z_BODY_TOP + H_DISK
for a in range(0, 360, 45):
    r = R_DISK_HOLES_AX if a % 90 == 0 else R_DISK_HOLES_DG
    x, y = r * math.cos(math.radians(a)), r * math.sin(math.radians(a))
    part = part.cut(cyl(DISK_HOLE_R, zd - DISK_HOLE_D, zd + 1).translate((x, y, 0)))

# centre tapered pocket (cone cut, extended above the face)
ext = 0.5
r_ext = CENTER_BOT_R + (CENTER_TOP_R - CENTER_BOT_R) * (CENTER_D + ext) / CENTER_D
cone = cq.Solid.makeCone(CENTER_BOT_R, r_ext, CENTER_D + ext,
                         cq.Vector(0, 0, zd - CENTER_D), cq.Vector(0, 0, 1))
cone = cone.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), SEAM_ANGLE)
part = part.cut(cq.Workplane("XY").add(cone))


result = part

VIEW = {"azimuth": 45, "elevation": 26}
